import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 46.0          # width  (X)
D = 22.7          # depth  (Y), front face at y = 0, back face at y = D
H = 60.0          # height (Z)
BACK = 1.8        # solid back plate thickness
SLOT_DEPTH = D - BACK

PITCH = 19.2      # vertical pitch of the three rows
SLOT_H = 8.37     # height of the horizontal through slots
SLOT1_Z0 = 44.94  # bottom of the top slot

# recess depth (from the front face) of every silhouette: inside a silhouette
# the material is removed in front of this depth and kept behind it, in the
# bands as well as across the slots (where it stands as an island)
CIRC_Y = 15.9     # circle, top row
RR1_Y = 4.0       # upper rounded rectangle, middle row
RR2_Y = 1.2       # lower rounded rectangle, bottom row
CONN_Y = 0.3      # shallow web between the two rectangles
LHEAD_Y = 14.1    # left heads
RHEAD_Y = SLOT_DEPTH  # right heads are open down to the back plate

CIRC_X, CIRC_Z, CIRC_R = 7.78, 49.42, 6.95
RR_X0, RR_X1, RR_R = 1.42, 14.3, 1.2
RR1_Z = (23.6, 35.9)
RR2_Z = (5.1, 16.8)
CONN_X1 = 13.45

HEAD_DX = 15.38   # x spacing of the two heads in a row
HEAD_X0 = 16.70   # neck bottom-left corner of the left head, top row
HEAD_Z0 = 41.03

# head silhouette facing -X (local coords, origin at neck bottom-left corner)
HEAD_PTS = [
    (0.50, 7.84), (0.20, 8.27), (-0.53, 8.73), (-1.04, 9.16), (-1.20, 9.59),
    (-1.10, 10.05), (-0.70, 10.40), (-0.75, 10.70), (-1.05, 11.10), (-0.95, 11.55),
    (-0.55, 11.95), (-0.25, 12.45), (0.15, 12.95), (0.70, 13.40), (0.55, 14.05),
    (0.42, 14.70), (0.45, 15.30), (0.75, 15.75), (1.45, 15.98), (2.10, 16.30),
    (2.65, 16.55), (3.15, 16.40), (3.63, 15.84), (4.15, 14.95), (4.59, 14.40),
    (5.20, 14.25), (6.09, 14.22), (7.26, 13.93), (8.43, 13.45), (9.42, 12.77),
    (10.20, 12.08), (10.96, 11.32), (11.57, 10.81), (12.54, 10.33), (13.15, 9.64),
    (12.95, 8.96), (12.16, 8.20), (10.79, 7.59), (9.62, 7.31), (9.21, 7.01),
]
NECK_TL = (0.50, 7.20)   # top of the straight left neck edge
NECK_BR = (10.35, 0.0)  # neck bottom-right corner


def prism_xz(sketch_fn, y0, y1):
    """Extrude an XZ profile so that it spans y0..y1."""
    wp = cq.Workplane("XZ", origin=(0, y1, 0))
    return sketch_fn(wp).extrude(y1 - y0)


def head_profile(ox, oz):
    def fn(wp):
        pts = [(ox + u, oz + v) for (u, v) in HEAD_PTS]
        return (wp.moveTo(ox, oz)
                .lineTo(ox + NECK_TL[0], oz + NECK_TL[1])
                .spline(pts, includeCurrent=True)
                .lineTo(ox + NECK_BR[0], oz + NECK_BR[1])
                .close())
    return fn


def circle_profile(wp):
    return wp.center(CIRC_X, CIRC_Z).circle(CIRC_R)


def rrect_profile(x0, x1, z0, z1, r):
    def fn(wp):
        return (wp.center((x0 + x1) / 2, (z0 + z1) / 2)
                .sketch().rect(x1 - x0, z1 - z0).vertices().fillet(r).finalize())
    return fn


def rect_profile(x0, x1, z0, z1):
    def fn(wp):
        return wp.center((x0 + x1) / 2, (z0 + z1) / 2).rect(x1 - x0, z1 - z0)
    return fn


# (profile, recess depth) for every silhouette
SILHOUETTES = [
    (circle_profile, CIRC_Y),
    (rrect_profile(RR_X0, RR_X1, RR1_Z[0], RR1_Z[1], RR_R), RR1_Y),
    (rrect_profile(RR_X0, RR_X1, RR2_Z[0], RR2_Z[1], RR_R), RR2_Y),
    (rect_profile(RR_X0, CONN_X1, RR2_Z[1], RR1_Z[0]), CONN_Y),
]
for row in range(3):
    oz = HEAD_Z0 - row * PITCH
    SILHOUETTES.append((head_profile(HEAD_X0, oz), LHEAD_Y))
    SILHOUETTES.append((head_profile(HEAD_X0 + HEAD_DX, oz), RHEAD_Y))


def union_all(shapes):
    out = shapes[0]
    for s in shapes[1:]:
        out = out.union(s, clean=False)
    return out


# ---------------- base block ----------------
block = cq.Workplane("XY").box(W, D, H, centered=False)

# three horizontal slots through the full width, down to the back plate
slots = union_all([
    cq.Workplane("XY").box(W, SLOT_DEPTH, SLOT_H, centered=False)
    .translate((0, 0, SLOT1_Z0 - row * PITCH))
    for row in range(3)
])

# silhouettes stay solid behind their recess depth (islands inside the slots)
islands = union_all([prism_xz(p, y, SLOT_DEPTH) for p, y in SILHOUETTES if y < SLOT_DEPTH - 1e-6])
part = block.cut(slots.cut(islands))

# ... and are pocketed in front of it (in the bands as well)
pockets = union_all([prism_xz(p, -1.0, y) for p, y in SILHOUETTES])
part = part.cut(pockets, clean=False)

result = part.translate((-W / 2, -D / 2, -H / 2))
